import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Sectioned cast bracket (half model, cut plane at X = 0)
#   X : across the part (X = 0 is the section plane, part lies at X < 0)
#   Y : along the part (Y = 0 front / end plate, Y = L back / frame)
#   Z : up
# ---------------------------------------------------------------------------

# ---- plates --------------------------------------------------------------
TP_BOT, TP_TOP = 30.4, 32.2        # top plate
RAISE_TOP = 34.0                   # raised pad of top plate around bore
RIB_TOP = 34.2                     # arc rib on top plate
BPF_BOT, BPF_TOP = 5.6, 9.0        # bottom plate, front (box) region (pad underside / top)
BPF_BOT_OUT = 6.7                  # underside of the floor outside the pad
BPB_BOT, BPB_TOP = 1.2, 2.4        # bottom plate, rear region
RAMP_Y0, RAMP_Y1 = 52.1, 60.5      # underside ramp between the two levels
RAMP_TOP_Y0, RAMP_TOP_Y1 = 58.3, 64.1   # top side of the ramp
FIN_X = (-46.3, -37.2)             # two thin fins under the ramp
FIN_T = 1.3
FIN_Z0 = 4.1                       # fin front edge bottom (at RAMP_Y0)

# ---- outline -------------------------------------------------------------
X_WALL = -48.1                     # straight outer side
Y_SIDE_END = 58.0                  # where the straight side turns to the lobe
Y_FRONT_L = 5.8                    # front edge at the outer side
FRONT_B = (-18.0, 0.0)             # second point defining the slanted front edge
CORNER_X = -13.8                   # x of the flat just before the bore
CORNER_R = 4.5                     # vertical round on the front corner
CORNER_BLOCK_X = -22.5             # solid corner post starts here (end plate abuts it)
Y_BACK = 97.75                     # rear edge of top plate at the cut
LOBE_C = (-54.8, 87.6)             # boss / lobe centre
LOBE_R = 9.6
BOSS_R = 6.5
SKIRT_A = (100.0, 215.0)           # outer skirt around the boss (deg)
LOBE_HOLE_R = 5.6

# ---- pad around the bore (raised on top, lowered underneath)
PAD_X = -27.1
PAD_C = (-1.7, 20.9)
PAD_R = 25.4

# ---- big bore (cut by section plane) -------------------------------------
BORE_C = (0.5, 17.6)
BORE_R = 17.7
BORE_R_BOT = 15.7                  # bore in the floor is a little smaller

BP_REAR = [(-43.0, 83.2), (-27.4, 84.6), (-7.4, 88.8)]   # floor rear edge

# ---- holes in plates -----------------------------------------------------
HOLES = [(-34.4, 74.2, 5.1), (-33.3, 42.5, 6.3), (-35.7, 18.9, 5.1)]
HOLE_RIM = 0.4                     # small 45 deg chamfer at the top of the holes
HALF_HOLES_Y = (41.6, 50.5)        # small bolt holes split by the section plane
HH_R, HH_CB_R, HH_CB_D = 1.0, 1.7, 1.4

# ---- walls ---------------------------------------------------------------
WALL_T = 1.8
Y_BACKWALL = 57.4
WIN_B = (9.0, 29.5)                # front window in the side wall (Y range), full height
WIN_R = 1.2                        # corner radius of the front window
WIN_A = (36.0, 14.8, 10.6, 24.5)   # rear window: y start, z bottom at start / at corner, z top
WIN_DIAG = 0.46                    # rear window runs on into the diagonal wall (fraction)

# ---- middle web ----------------------------------------------------------
MID_Z0, MID_Z1 = 19.3, 20.7
MID_X0 = -12.0
COL_X = (X_WALL + WALL_T - 0.2, -10.9)   # transverse web behind the bore
COL_Y = (33.3, 34.6)
COL_WIN = (-35.1, -22.5, 10.5, 27.0)     # window in that web (x0, x1, z0, z1)
COL_SLOT = (-20.1, -18.1)                # narrow full-height slot in that web

# ---- end plate -----------------------------------------------------------
EP_Y0, EP_Y1 = 3.5, 5.9
EP_X0, EP_X1 = -62.7, -22.5
EP_Z0, EP_Z1 = 8.5, 31.0
EP_HOLE = (-58.7, 26.1, 1.3)

# ---- rear frame ----------------------------------------------------------
FR_X0 = -7.4
FR_Y_END = 118.3
FR_Z_KNEE = 8.2
FR_T = 1.5


def pol(c, r, deg):
    return (c[0] + r * math.cos(math.radians(deg)), c[1] + r * math.sin(math.radians(deg)))


def lobe_tangent(p, c, r):
    """left tangent point from external point p to circle (c, r)"""
    dx, dy = c[0] - p[0], c[1] - p[1]
    d = math.hypot(dx, dy)
    a = math.atan2(dy, dx) + math.asin(r / d)
    L = math.sqrt(d * d - r * r)
    return (p[0] + L * math.cos(a), p[1] + L * math.sin(a))


T_LEFT = lobe_tangent((X_WALL, Y_SIDE_END), LOBE_C, LOBE_R)
A_LEFT = math.degrees(math.atan2(T_LEFT[1] - LOBE_C[1], T_LEFT[0] - LOBE_C[0])) % 360

# front corner: vertical round between the slanted front edge and the flat x = CORNER_X
_A = (X_WALL, Y_FRONT_L)
_dx, _dy = FRONT_B[0] - _A[0], FRONT_B[1] - _A[1]
_L = math.hypot(_dx, _dy)
_d = (_dx / _L, _dy / _L)
_n = (-_d[1], _d[0])                      # inward normal (+Y side)
_cx = CORNER_X - CORNER_R
_cy = _A[1] + (CORNER_R - _n[0] * (_cx - _A[0])) / _n[1]
CORNER_P0 = (_cx - CORNER_R * _n[0], _cy - CORNER_R * _n[1])
CORNER_P1 = (CORNER_X, _cy)
_m = (1.0 - _n[0], -_n[1])
_ml = math.hypot(*_m)
CORNER_MID = (_cx + CORNER_R * _m[0] / _ml, _cy + CORNER_R * _m[1] / _ml)


def outline_wp(z0):
    """plan outline of the plates (before the bore is cut) as a closed wire"""
    return (
        cq.Workplane("XY", origin=(0, 0, z0))
        .moveTo(0, Y_BACK)
        .lineTo(-7.4, Y_BACK)
        .lineTo(-20.2, 91.0)
        .lineTo(-37.7, 87.6)
        .threePointArc((-42.3, 89.4), pol(LOBE_C, LOBE_R, 40))
        .threePointArc(pol(LOBE_C, LOBE_R, (40 + A_LEFT) / 2), T_LEFT)
        .lineTo(X_WALL, Y_SIDE_END)
        .lineTo(X_WALL, Y_FRONT_L)
        .lineTo(*CORNER_P0)
        .threePointArc(CORNER_MID, CORNER_P1)
        .lineTo(CORNER_X, 8.0)
        .lineTo(0, 8.0)
        .close()
    )


def outline(z0, z1):
    return outline_wp(z0).extrude(z1 - z0)


def cyl(cx, cy, r, z0, z1):
    return cq.Workplane("XY", origin=(0, 0, z0)).center(cx, cy).circle(r).extrude(z1 - z0)


def vol(wp):
    return sum(sol.Volume() for sol in wp.solids().vals())


def safe_union(a, b):
    """boolean union with a sanity check; retry with a fuzzy tolerance if OCC misbehaves"""
    va, vb = vol(a), vol(b)
    r = a.union(b)
    vr = vol(r)
    if vr < max(va, vb) * 0.999 or vr > (va + vb) * 1.001:
        r = a.union(b, tol=1e-3)
    return r


def box(x0, x1, y0, y1, z0, z1):
    return (
        cq.Workplane("XY")
        .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
        .translate((x0, y0, z0))
    )


# ---------------------------------------------------------------- top plate
top = outline(TP_BOT, TP_TOP)

# raised pad around the bore (bounded by a rounded line on the plate)
def pad(z0, z1):
    prof = (
        cq.Workplane("XY", origin=(0, 0, z0))
        .moveTo(0, -2)
        .lineTo(PAD_X, -2)
        .lineTo(PAD_X, PAD_C[1])
        .threePointArc(pol(PAD_C, PAD_R, 135), (PAD_C[0], PAD_C[1] + PAD_R))
        .lineTo(0, PAD_C[1] + PAD_R)
        .close()
        .extrude(z1 - z0)
    )
    return prof.intersect(outline(z0, z1))


top = top.union(pad(TP_TOP, RAISE_TOP))

# arc rib concentric with the bore
r_in, r_out = 48.8, 57.7
rib = (
    cq.Workplane("XY", origin=(0, 0, TP_TOP))
    .moveTo(*pol(BORE_C, r_in, 90))
    .lineTo(*pol(BORE_C, r_out, 90))
    .threePointArc(pol(BORE_C, r_out, 105), pol(BORE_C, r_out, 120))
    .lineTo(*pol(BORE_C, r_in, 124))
    .threePointArc(pol(BORE_C, r_in, 107), pol(BORE_C, r_in, 90))
    .close()
    .extrude(RIB_TOP - TP_TOP)
)
# round the free end of the rib
rib = rib.edges("|Z").edges(cq.selectors.BoxSelector((-60, 40, 0), (-10, 90, 40))).fillet(1.8)
top = top.union(rib)
top = top.cut(cyl(BORE_C[0], BORE_C[1], BORE_R, TP_BOT - 1, RIB_TOP + 1))

# ---------------------------------------------------------------- bottom plate
bot_raw = outline(BPB_BOT, BPF_TOP)
bot_raw = bot_raw.union(box(FR_X0, 0, 60, FR_Y_END, BPB_BOT, BPB_TOP))
step = (
    cq.Workplane("YZ", origin=(-70, 0, 0))
    .polyline([
        (-5, BPF_BOT_OUT), (RAMP_Y0, BPF_BOT_OUT), (RAMP_Y1, BPB_BOT),
        (125, BPB_BOT), (125, BPB_TOP), (RAMP_TOP_Y1, BPB_TOP), (RAMP_TOP_Y0, BPF_TOP),
        (-5, BPF_TOP),
    ])
    .close()
    .extrude(80)
)
bottom = bot_raw.intersect(step)
# rear edge of the floor sits in front of the top plate rear edge
rear_cut = (
    cq.Workplane("XY", origin=(0, 0, -1))
    .polyline([BP_REAR[2], BP_REAR[1], BP_REAR[0], (-50.0, BP_REAR[0][1]),
               (-50.0, 101.0), (FR_X0, 101.0)])
    .close()
    .extrude(6)
)
bottom = bottom.cut(rear_cut).union(cyl(LOBE_C[0], LOBE_C[1], LOBE_R, BPB_BOT, BPB_TOP))
bottom = bottom.union(pad(BPF_BOT, BPF_BOT_OUT + 0.1))
for fx in FIN_X:
    fin = (
        cq.Workplane("YZ", origin=(fx - FIN_T / 2, 0, 0))
        .polyline([(RAMP_Y0, BPF_BOT_OUT + 0.5), (RAMP_Y0, FIN_Z0), (61.4, BPB_BOT),
                   (62.5, BPB_BOT + 0.5), (62.5, BPF_BOT_OUT + 0.5)])
        .close()
        .extrude(FIN_T)
    )
    bottom = bottom.union(fin)
bottom = bottom.cut(cyl(BORE_C[0], BORE_C[1], BORE_R_BOT, -1, BPF_TOP + 1))

# ---------------------------------------------------------------- boss (with flared foot)
boss = (
    cq.Workplane("XZ")
    .moveTo(0, BPB_BOT)
    .lineTo(LOBE_R - 0.4, BPB_BOT)
    .lineTo(LOBE_R - 0.4, BPB_TOP)
    .threePointArc((BOSS_R + 0.8, BPB_TOP + 1.1), (BOSS_R, BPB_TOP + 3.8))
    .lineTo(BOSS_R, TP_TOP)
    .lineTo(0, TP_TOP)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .translate((LOBE_C[0], LOBE_C[1], 0))
)

a0, a1 = SKIRT_A
skirt = (
    cq.Workplane("XY", origin=(0, 0, BPB_BOT))
    .moveTo(*pol(LOBE_C, BOSS_R - 0.5, a0))
    .lineTo(*pol(LOBE_C, LOBE_R, a0))
    .threePointArc(pol(LOBE_C, LOBE_R, (a0 + a1) / 2), pol(LOBE_C, LOBE_R, a1))
    .lineTo(*pol(LOBE_C, BOSS_R - 0.5, a1))
    .threePointArc(pol(LOBE_C, BOSS_R - 0.5, (a0 + a1) / 2), pol(LOBE_C, BOSS_R - 0.5, a0))
    .close()
    .extrude(TP_TOP - BPB_BOT)
)
boss = safe_union(boss, skirt)

# ---------------------------------------------------------------- walls
side = box(X_WALL, X_WALL + WALL_T, Y_FRONT_L, Y_SIDE_END, BPF_BOT, TP_BOT + 0.1)
win_b = box(X_WALL - 1, X_WALL + 3, WIN_B[0], WIN_B[1], BPF_TOP - 0.2, TP_BOT + 0.2)
side = side.cut(win_b.edges("|X").fillet(WIN_R))
win_a = (
    cq.Workplane("YZ", origin=(X_WALL - 1, 0, 0))
    .polyline([(WIN_A[0], WIN_A[1]), (Y_SIDE_END + 1, WIN_A[2]),
               (Y_SIDE_END + 1, WIN_A[3]), (WIN_A[0], WIN_A[3])])
    .close()
    .extrude(4)
)
side = side.cut(win_a)

# diagonal wall from the side wall to the boss (outer face on the outline)
dx, dy = T_LEFT[0] - X_WALL, T_LEFT[1] - Y_SIDE_END
dlen = math.hypot(dx, dy)
ang = math.degrees(math.atan2(dy, dx))


def along_diag(shape):
    return shape.rotate((0, 0, 0), (0, 0, 1), ang).translate((X_WALL, Y_SIDE_END, 0))


DIAG_T = 3.0
diag = along_diag(
    cq.Workplane("XY")
    .box(dlen, DIAG_T, TP_BOT - BPB_BOT, centered=False)
    .translate((0, -DIAG_T, BPB_BOT))
)
# the wall continues the rear side window
diag = diag.cut(
    along_diag(
        cq.Workplane("XY")
        .box(dlen * WIN_DIAG + 1.0, 6, WIN_A[3] - 9.2, centered=False)
        .translate((-1.0, -3, 9.2))
    )
)

backwall = box(X_WALL, 0, Y_BACKWALL, Y_BACKWALL + 1.0, BPF_BOT + 1.0, TP_BOT + 0.1)

# ---------------------------------------------------------------- middle web + column
mid = box(MID_X0, 0, 33.0, Y_BACKWALL + 0.5, MID_Z0, MID_Z1)
mid = mid.cut(cyl(0, 51.3, 5.7, MID_Z0 - 1, MID_Z1 + 1))
column = box(COL_X[0], COL_X[1], COL_Y[0], COL_Y[1], BPF_TOP - 0.5, TP_BOT + 0.5)
column = column.cut(box(COL_WIN[0], COL_WIN[1], COL_Y[0] - 1, COL_Y[1] + 1, COL_WIN[2], COL_WIN[3]))
column = column.cut(box(COL_SLOT[0], COL_SLOT[1], COL_Y[0] - 1, COL_Y[1] + 1, BPF_TOP, TP_BOT))

# ---------------------------------------------------------------- front corner post
corner = outline(BPF_BOT, RAISE_TOP).intersect(box(CORNER_BLOCK_X, 0, -2, 8.5, BPF_BOT, RAISE_TOP))

# ---------------------------------------------------------------- end plate
ep = (
    cq.Workplane("XZ", origin=(0, EP_Y1, 0))
    .moveTo(EP_X1, EP_Z0)
    .lineTo(EP_X1, EP_Z1)
    .lineTo(EP_X0 + 2.0, EP_Z1)
    .threePointArc((EP_X0 + 0.586, EP_Z1 - 0.586), (EP_X0, EP_Z1 - 2.0))
    .lineTo(EP_X0, 20.1)
    .lineTo(-48.2, EP_Z0)
    .close()
    .extrude(EP_Y1 - EP_Y0)
)
ep = ep.cut(
    cq.Workplane("XZ", origin=(0, EP_Y1 + 1, 0))
    .center(EP_HOLE[0], EP_HOLE[1])
    .circle(EP_HOLE[2])
    .extrude(5)
)

# ---------------------------------------------------------------- rear frame
FR_STEP_Y = 87.0                   # frame foot bar (thicker, down to Z = 0) starts here
FR_BAR_TOP = 2.8
frame_outer = [
    (FR_STEP_Y, TP_TOP), (Y_BACK - 0.45, TP_TOP), (FR_Y_END, FR_Z_KNEE), (FR_Y_END, 0.0),
    (FR_STEP_Y, 0.0)
]
FR_FIL = 2.2                       # inner round at the foot of the frame end
_yi = FR_Y_END - FR_T
frame = cq.Workplane("YZ", origin=(FR_X0, 0, 0)).polyline(frame_outer).close().extrude(-FR_X0)
frame_win = (
    cq.Workplane("YZ", origin=(FR_X0 - 1, 0, 0))
    .moveTo(FR_STEP_Y - 1.0, TP_BOT)
    .lineTo(Y_BACK - 1.3, TP_BOT)
    .lineTo(_yi, FR_Z_KNEE + 0.6)
    .lineTo(_yi, FR_BAR_TOP + FR_FIL)
    .threePointArc((_yi - FR_FIL * (1 - 0.7071), FR_BAR_TOP + FR_FIL * (1 - 0.7071)),
                   (_yi - FR_FIL, FR_BAR_TOP))
    .lineTo(FR_STEP_Y, FR_BAR_TOP)
    .lineTo(FR_STEP_Y, BPB_TOP)
    .lineTo(FR_STEP_Y - 1.0, BPB_TOP)
    .close()
    .extrude(-FR_X0 + 2)
)
frame = frame.cut(frame_win)

# ---------------------------------------------------------------- assemble
inner = side
for part in (diag, backwall, mid, column, corner):
    inner = safe_union(inner, part)
inner = inner.cut(cyl(BORE_C[0], BORE_C[1], BORE_R, -1, 40))

body = top
for part in (bottom, boss, inner, ep, frame):
    body = safe_union(body, part)

# lobe hole and plate holes
body = body.cut(cyl(LOBE_C[0], LOBE_C[1], LOBE_HOLE_R, -1, 40))
for hx, hy, hr in HOLES:
    body = body.cut(cyl(hx, hy, hr, -1, 40))
    cone = cq.Solid.makeCone(hr, hr + HOLE_RIM + 0.5, HOLE_RIM + 0.5,
                             cq.Vector(hx, hy, TP_TOP - HOLE_RIM), cq.Vector(0, 0, 1))
    body = body.cut(cq.Workplane("XY").add(cone))

# half holes on the section plane (top and bottom plates), counterbored from inside
for hy in HALF_HOLES_Y:
    body = body.cut(cyl(0, hy, HH_R, TP_BOT - 1.0, 40))
    body = body.cut(cyl(0, hy, HH_CB_R, TP_BOT - 1.0, TP_BOT + HH_CB_D))
    body = body.cut(cyl(0, hy, HH_R, -1, BPF_TOP + 1.0))
    body = body.cut(cyl(0, hy, HH_CB_R, BPF_TOP - HH_CB_D, BPF_TOP + 1.0))

# trim anything beyond the section plane
body = body.intersect(box(-80, 0, -5, 130, -5, 40))

result = body
